import math
import cadquery as cq

# ---------------------------------------------------------------
# Laser range scanner on a U-shaped tilt bracket (all mm)
# X: right, Y: depth, Z: up.  z = 0 is underside of bracket plate
# ---------------------------------------------------------------

# bracket
BP_X = 31.4        # half size of base plate along X
BP_T = 2.6         # base plate thickness
ARM_X = 19.0       # half width of the side arms
ARM_T = 2.3        # arm thickness
ARM_H = 25.0       # arm height
ARM_Y = 43.7       # outer face of arms
BP_Y = 41.2        # half size of base plate along Y (outside the arms)
BOSS_D = 7.0       # pivot bolt head diameter
BOSS_X = 6.25      # pivot bolts +-X
BOSS_Z = 19.0      # pivot bolt height
BOSS_L = 3.8       # bolt head length

# lower housing
LB_H = 37.6        # half size lower box
LB_Z0 = 6.6
LB_Z1 = 27.7
SP_Y = 41.4        # side covers (+-Y) outer face
FL_H = 38.5        # flange half size
FL_Z1 = 30.75
FIN_N = 8          # heat sink grooves on the +X face
FIN_PITCH = 8.4
FIN_WT = 2.6       # groove width at top
FIN_WB = 4.5       # groove width at bottom
FIN_ZT = 26.6      # groove top
STEP_H = 2.6       # bottom cover step height
FIN_DEPTH = 2.0

# middle housing
MB_H = 36.75
MB_Z1 = 57.0       # start of top bevel
MB_TOP = 61.1
MB_IN = 31.0       # half size of top face
MB_IN_R = 18.0     # plan corner radius of top face
CH_C = 33.3        # bottom screw axis (in the corner channel)
CH_IN = 29.3       # corner channel walls
CH_R = 3.9         # rounding of the channel back
CH_Z0 = 33.0       # floor of the corner channel (bottom screw seat)
TS_C = 25.6        # top screw position
TS_Z0 = 58.6       # top screw seat
SCREW_D = 4.6

# optical window (frustum) and rear block
CONE_R0 = 30.6
CONE_R1 = 27.6
CONE_Z1 = 97.2
REAR_X0 = 35.0     # rear face at bottom
REAR_X1 = 33.9     # rear face at top
REAR_YN = -5.0     # rear face spans REAR_YN .. REAR_YP
REAR_YP = 13.0

# cap
CAP_Z0 = 96.6
CAP_ZP = 108.9     # parting line
CAP_TOP = 118.5
CAP_H = 34.3       # half size of cap outline
CAP_R = 17.0       # plan corner radius of cap outline
CORE_H = 30.4      # half size of recessed core between lobes
LOBE_IN = 14.3     # lobes start at this distance from the axes
PILL_Z0 = 103.4
PILL_OUT = 35.3    # bumpers stand slightly proud of the lobes
PILL_Z1 = 115.7
CAP_IND = 28.2     # top plate indent between lobes
TOP_Z0 = 112.5     # underside of the top plate
TOP_FIL = 4.5      # rounding of the top plate
LOBE_C = 23.6
LABEL = 29.0

# cables
CAB_Y = 18.6
CAB_Z = 17.6
CAB_D = 7.0
CAB_L = 62.5       # x of cable end (negative side)
GL_D0 = 12.0
GL_D1 = 8.0
GL_L = 6.0


def box(x0, x1, y0, y1, z0, z1):
    return cq.Workplane("XY").box(x1 - x0, y1 - y0, z1 - z0, centered=False).translate((x0, y0, z0))


def cyl(r, h, pnt, d):
    return cq.Workplane("XY").add(cq.Solid.makeCylinder(r, h, cq.Vector(*pnt), cq.Vector(*d)))


def rrect(hx, hy, r, z0, z1):
    return (cq.Workplane("XY").workplane(offset=z0).rect(2 * hx, 2 * hy)
            .extrude(z1 - z0).edges("|Z").fillet(r))


def rounded_wire(pts, z=0.0):
    """closed polygon [(x, y, r), ...] with a corner fillet of radius r at each vertex"""
    n = len(pts)
    segs = []
    for i in range(n):
        px, py, r = pts[i]
        ax, ay, _ = pts[i - 1]
        bx, by, _ = pts[(i + 1) % n]
        u1 = (ax - px, ay - py)
        l1 = math.hypot(*u1)
        u1 = (u1[0] / l1, u1[1] / l1)
        u2 = (bx - px, by - py)
        l2 = math.hypot(*u2)
        u2 = (u2[0] / l2, u2[1] / l2)
        th = math.acos(max(-1.0, min(1.0, u1[0] * u2[0] + u1[1] * u2[1]))) / 2
        if r <= 0 or abs(th - math.pi / 2) < 1e-9:
            segs.append(((px, py), None, (px, py)))
            continue
        d = r / math.tan(th)
        t1 = (px + u1[0] * d, py + u1[1] * d)
        t2 = (px + u2[0] * d, py + u2[1] * d)
        bv = (u1[0] + u2[0], u1[1] + u2[1])
        lb = math.hypot(*bv)
        bv = (bv[0] / lb, bv[1] / lb)
        hc = r / math.sin(th)
        c = (px + bv[0] * hc, py + bv[1] * hc)
        m = (c[0] - bv[0] * r, c[1] - bv[1] * r)
        segs.append((t1, m, t2))
    wp = cq.Workplane("XY").workplane(offset=z).moveTo(*segs[0][0])
    for i, (t1, m, t2) in enumerate(segs):
        if i > 0:
            wp = wp.lineTo(*t1)
        if m is not None:
            wp = wp.threePointArc(m, t2)
    return wp.close()


def rounded_poly(pts, z0, z1):
    return rounded_wire(pts, z0).extrude(z1 - z0)


def rsq_pts(h, r):
    return [(h, h, r), (-h, h, r), (-h, -h, r), (h, -h, r)]


def mirror4(shape):
    """copy a +X+Y corner feature into all four quadrants"""
    out = shape.union(shape.mirror("YZ"))
    return out.union(out.mirror("XZ"))


def socket_screw(x, y, z, d, h, axis="Z"):
    """socket head cap screw head standing on point (x,y,z) along axis"""
    if axis == "Z":
        s = cyl(d / 2, h, (x, y, z), (0, 0, 1))
        s = s.faces(">Z").edges().fillet(d * 0.08)
        hexcut = (cq.Workplane("XY").workplane(offset=z + h * 0.45)
                  .center(x, y).polygon(6, d * 0.5).extrude(h))
    else:
        sgn = 1 if axis == "+Y" else -1
        s = cyl(d / 2, h, (x, y, z), (0, sgn, 0))
        s = s.faces(">Y" if sgn > 0 else "<Y").edges().fillet(d * 0.08)
        wp = cq.Workplane("XZ", origin=(0, y + sgn * h * 0.45, 0))
        hexcut = wp.center(x, z).polygon(6, d * 0.5).extrude(-sgn * h)
    return s.cut(hexcut)


# ---------------- bracket ----------------
bracket = box(-BP_X, BP_X, -BP_Y, BP_Y, 0, BP_T)
bracket = bracket.edges("|Z").fillet(2.0)
bracket = bracket.union(box(-ARM_X, ARM_X, -ARM_Y, ARM_Y, 0, BP_T))
for sx in (-1, 1):
    for sy in (-1, 1):
        bracket = bracket.cut(cyl(1.7, BP_T + 2, (sx * (BP_X - 4.5), sy * (BP_Y - 6.0), -1), (0, 0, 1)))
for sy in (-1, 1):
    y0 = ARM_Y - ARM_T if sy > 0 else -ARM_Y
    arm = box(-ARM_X, ARM_X, y0, y0 + ARM_T, 0, ARM_H)
    arm = arm.edges("|Y and >Z").fillet(0.6)
    # tilt slot between the two pivot bolts
    slot = (cq.Workplane("XZ", origin=(0, sy * (ARM_Y + 1.0), 0)).center(0, BOSS_Z)
            .slot2D(2 * BOSS_X + 2.6, 2.6, 0).extrude(1.8 if sy > 0 else -1.8))
    bracket = bracket.union(arm).cut(slot)
    for sx in (-1, 1):
        bracket = bracket.union(
            socket_screw(sx * BOSS_X, sy * (ARM_Y - 0.9), BOSS_Z, BOSS_D, BOSS_L + 0.9, "+Y" if sy > 0 else "-Y"))

# ---------------- lower housing ----------------
lower = box(-LB_H, LB_H, -LB_H, LB_H, LB_Z0, LB_Z1)
# bottom cover step
step = box(-LB_H - 1, LB_H + 1, -LB_H - 1, LB_H + 1, LB_Z0 - 1, LB_Z0 + STEP_H).cut(
    box(-LB_H + 0.8, LB_H - 0.8, -LB_H + 0.8, LB_H - 0.8, LB_Z0 - 2, LB_Z0 + STEP_H + 1))
lower = lower.cut(step)


def groove(yc, sx):
    """tapered vertical heat-sink groove in the +-X face of the lower box"""
    zb, zt = LB_Z0 + STEP_H - 0.01, FIN_ZT
    pts = [(yc - FIN_WB / 2, zb), (yc + FIN_WB / 2, zb), (yc + FIN_WT / 2, zt), (yc - FIN_WT / 2, zt)]
    sk = cq.Workplane("YZ", origin=(sx * (LB_H + 1), 0, 0)).polyline(pts).close()
    return sk.extrude(-sx * (FIN_DEPTH + 1))


for sx in (-1, 1):
    if sx > 0:
        ys = [FIN_PITCH * (i - (FIN_N - 1) / 2) for i in range(FIN_N)]
    else:
        ys = [-FIN_PITCH * 3.5, -FIN_PITCH * 0.5, FIN_PITCH * 0.5, FIN_PITCH * 3.5]
    for yy in ys:
        lower = lower.cut(groove(yy, sx))

# side covers (+-Y) with bevelled edges
for sy in (-1, 1):
    y0 = LB_H - 0.2 if sy > 0 else -SP_Y
    cov = box(-LB_H, LB_H, y0, y0 + (SP_Y - LB_H + 0.2), LB_Z0 + STEP_H, LB_Z1)
    cov = cov.faces(">Y" if sy > 0 else "<Y").edges().chamfer(1.0)
    lower = lower.union(cov)
# flange
flange = box(-FL_H, FL_H, -FL_H, FL_H, LB_Z1, FL_Z1).edges("|Z").fillet(1.5)
lower = lower.union(flange)
# bottom screws of the sensor
for sx in (-1, 1):
    for sy in (-1, 1):
        lower = lower.union(cyl(2.0, 1.0, (sx * 31.0, sy * 31.0, LB_Z0 - 1.0), (0, 0, 1)))

# cable glands and cables (-X side)
for sy in (-1, 1):
    g = cq.Workplane("XY").add(cq.Solid.makeCone(GL_D0 / 2, GL_D1 / 2, GL_L,
                                                cq.Vector(-LB_H + 0.5, sy * CAB_Y, CAB_Z),
                                                cq.Vector(-1, 0, 0)))
    lower = lower.union(g)
    lower = lower.union(cyl(CAB_D / 2, CAB_L - LB_H, (-LB_H, sy * CAB_Y, CAB_Z), (-1, 0, 0)))

# ---------------- middle housing ----------------
mid = box(-MB_H, MB_H, -MB_H, MB_H, FL_Z1 - 0.01, MB_Z1)
bevel = cq.Workplane("XY").add(cq.Solid.makeLoft(
    [rounded_wire(rsq_pts(MB_H, 5.0), MB_Z1).val(), rounded_wire(rsq_pts(MB_IN, MB_IN_R), MB_TOP).val()], True))
mid = mid.union(bevel)
# corner channels: bottom screws sit on a ledge, top screws in a landing
d45 = math.sqrt(0.5)
chan = rounded_poly([(CH_IN, CH_IN, CH_R), (MB_H + 3, CH_IN, 0), (MB_H + 3, MB_H + 3, 0), (CH_IN, MB_H + 3, 0)],
                    CH_Z0, MB_TOP + 1)
land = (cq.Workplane("XY").workplane(offset=TS_Z0)
        .center(TS_C + 6 * d45, TS_C + 6 * d45).slot2D(12 + 2 * 3.6, 2 * 3.6, 45)
        .extrude(MB_TOP + 1 - TS_Z0))
mid = mid.cut(mirror4(chan.union(land)))
scr = socket_screw(CH_C, CH_C, CH_Z0, SCREW_D, 3.0).union(socket_screw(TS_C, TS_C, TS_Z0, SCREW_D, 2.4))
mid = mid.union(mirror4(scr))

# ---------------- window + rear block ----------------
cone = cq.Workplane("XY").add(cq.Solid.makeCone(CONE_R0, CONE_R1, CONE_Z1 - (MB_TOP - 0.3),
                                               cq.Vector(0, 0, MB_TOP - 0.3), cq.Vector(0, 0, 1)))
zr0, zr1 = MB_TOP - 0.3, CONE_Z1


def rear_wire(xr, z):
    """rear block section: flat rear face, 45 deg side running into the window"""
    w = REAR_YP - REAR_YN
    return cq.Wire.makePolygon([cq.Vector(-xr, REAR_YN, z), cq.Vector(-xr, REAR_YP, z),
                                cq.Vector(-xr + w - 4.0, REAR_YN + 4.0, z),
                                cq.Vector(-xr + w - 4.0, REAR_YN, z)], close=True)


rear = cq.Workplane("XY").add(cq.Solid.makeLoft([rear_wire(REAR_X0, zr0), rear_wire(REAR_X1, zr1)], True))
window = cone.union(rear)

# ---------------- cap ----------------
# lower body: recessed core + four corner lobes
core = rrect(CORE_H, CORE_H, 9.0, CAP_Z0 + 0.2, TOP_Z0 + 1.0)
lobe_pts = [(LOBE_IN, LOBE_IN, 3.0), (CAP_H, LOBE_IN, 2.5), (CAP_H, CAP_H, CAP_R), (LOBE_IN, CAP_H, 2.5)]
lobe = rounded_poly(lobe_pts, CAP_Z0, TOP_Z0)
lobe = lobe.faces("<Z").edges().fillet(3.0)
cap = core.union(mirror4(lobe))
# plain rear wall on the -X (cable) side instead of a bumper
rwall = box(-CAP_H, -CORE_H + 1.0, -LOBE_IN - 1.0, LOBE_IN + 1.0, CAP_Z0, TOP_Z0)
rwall = rwall.faces("<Z").edges("|Y").edges("<X").fillet(3.0)
cap = cap.union(rwall)
# rolled side bumpers between the lobes
pill_prof = [(CORE_H - 1.5, PILL_Z0, 0.0), (PILL_OUT, PILL_Z0, 3.6), (PILL_OUT, PILL_Z1, 3.6), (CORE_H - 1.5, PILL_Z1, 0.0)]
pill = rounded_poly(pill_prof, -LOBE_IN + 0.2, LOBE_IN - 0.2).rotate((0, 0, 0), (1, 0, 0), 90)
pill = pill.faces("<Y").edges().fillet(2.6).faces(">Y").edges().fillet(2.6)
cap = cap.union(pill).union(pill.rotate((0, 0, 0), (0, 0, 1), 90)).union(pill.rotate((0, 0, 0), (0, 0, 1), -90))
# top plate: cap outline indented between the lobes
H, I, Eo, Ei = CAP_H, CAP_IND, LOBE_IN + 0.2, LOBE_IN - 4.8
top_pts = []
for a in range(4):
    ca, sa = round(math.cos(a * math.pi / 2)), round(math.sin(a * math.pi / 2))
    side = [(Eo, H, 4.0), (Ei, I, 4.0), (-Ei, I, 4.0), (-Eo, H, 4.0)] if a != 1 else []
    for (px, py, pr) in [(H, H, CAP_R)] + side:
        top_pts.append((ca * px - sa * py, sa * px + ca * py, pr))
top = rounded_poly(top_pts, TOP_Z0, CAP_TOP).faces(">Z").edges().fillet(TOP_FIL)
cap = cap.union(top)
# parting line groove
groove_ring = rrect(CAP_H + 2, CAP_H + 2, CAP_R + 2, CAP_ZP - 0.2, CAP_ZP + 0.2).cut(
    rrect(CAP_H - 0.5, CAP_H - 0.5, CAP_R - 0.5, CAP_ZP - 1, CAP_ZP + 1))
cap = cap.cut(groove_ring)
# label pad on top
cap = cap.union(rrect(LABEL / 2, LABEL / 2, 2.0, CAP_TOP - 0.2, CAP_TOP + 0.5))
# counterbored lobe screws (cross recess)
for sx in (-1, 1):
    for sy in (-1, 1):
        cx, cy = sx * LOBE_C, sy * LOBE_C
        cap = cap.cut(cyl(4.2, 3.0, (cx, cy, CAP_TOP - 1.8), (0, 0, 1)))
        cap = cap.union(cyl(2.4, 1.0, (cx, cy, CAP_TOP - 1.9), (0, 0, 1)))
        cross = box(cx - 1.3, cx + 1.3, cy - 0.35, cy + 0.35, CAP_TOP - 1.3, CAP_TOP).union(
            box(cx - 0.35, cx + 0.35, cy - 1.3, cy + 1.3, CAP_TOP - 1.3, CAP_TOP))
        cap = cap.cut(cross)
# indicator window with two LEDs on the +X side of the cap skirt
cap = cap.union(box(CORE_H - 0.5, CORE_H + 0.8, -7.7, 7.7, 99.2, 102.4).edges("|X").fillet(1.2))
for yy in (-4.4, 4.4):
    cap = cap.cut(cyl(1.1, 1.0, (CORE_H + 0.4, yy, 100.8), (1, 0, 0)))

result = bracket.union(lower).union(mid).union(window).union(cap)
